import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 8.3            # plate / bar thickness
R_OUT = 31.4       # distance from centre to the outer face of each bar
BAR_W = 10.1       # bar width (radial)
BAR_L = 41.2       # bar length, end face to end face
END_R = 2.6        # radius of the flat end face of each bar
CONE_ANG = 31.0    # half angle of the conical bar ends (deg)
BAR_HOLE_D = 3.4   # through hole along each bar
NOTCH_W = 12.8     # gap between the two arms of a pair
NOTCH_D = 9.5      # depth of that gap (from the bar outer face)
NOTCH_R = 1.1      # edge round inside the gap
NOTCH_CR = 1.5     # corner round at the back of the gap
NUT_AF = 6.0       # hex nut trap across flats
NUT_DEPTH = 3.0    # hex nut trap depth
ARC_C = 40.7       # centre distance of the three concave cut-outs
ARC_R = 18.5       # radius of the concave cut-outs
EDGE_R = 1.2       # edge round on the concave outline
POCKET_D = 17.3    # two blind pockets on top
POCKET_DEPTH = 5.4
POCKET_X = 12.7
CENTER_HOLE_D = 3.4
SMALL_HOLE_D = 3.2
SMALL_HOLE_R = 21.7

PAIR_ANGLES = [60.0, 180.0, 300.0]    # outward normals of the three bars
ARC_ANGLES = [0.0, 120.0, 240.0]      # concave cut-out directions

R_C = R_OUT - BAR_W / 2.0             # bar axis distance from centre
ZC = H / 2.0
TAN_C = math.tan(math.radians(CONE_ANG))


def to_local(p, ang):
    """global point -> (u, v, z) in the frame of the bar whose normal is ang"""
    c, s = math.cos(math.radians(ang)), math.sin(math.radians(ang))
    return (p.x * c + p.y * s, -p.x * s + p.y * c, p.z)


# ---------------- central core ----------------
core_in = R_C
tri_r = 2.0 * core_in
tri_pts = [(tri_r * math.cos(math.radians(a)), tri_r * math.sin(math.radians(a)))
           for a in ARC_ANGLES]
core = cq.Workplane("XY").polyline(tri_pts).close().extrude(H)
for a in ARC_ANGLES:
    cx = ARC_C * math.cos(math.radians(a))
    cy = ARC_C * math.sin(math.radians(a))
    cutter = cq.Workplane("XY").center(cx, cy).circle(ARC_R).extrude(H)
    core = core.cut(cutter)
core = core.edges("%CIRCLE").fillet(EDGE_R)


# ---------------- one bar (local: outward normal +X, axis along Y) ----------------
def make_bar():
    rr = H / 2.0
    prof = (cq.Workplane("XZ", origin=(0, BAR_L / 2.0, 0))
            .moveTo(R_OUT - BAR_W, 0)
            .lineTo(R_OUT - rr, 0)
            .threePointArc((R_OUT, rr), (R_OUT - rr, H))
            .lineTo(R_OUT - BAR_W, H)
            .close()
            .extrude(BAR_L))
    # conical end caps around the bar axis
    r_big = 9.0
    hc = (r_big - END_R) / TAN_C
    c1 = cq.Solid.makeCone(END_R, r_big, hc, cq.Vector(R_C, -BAR_L / 2.0, ZC),
                           cq.Vector(0, 1, 0))
    c2 = cq.Solid.makeCone(END_R, r_big, hc, cq.Vector(R_C, BAR_L / 2.0, ZC),
                           cq.Vector(0, -1, 0))
    mid = cq.Solid.makeCylinder(r_big, BAR_L - 2 * hc + 0.02,
                                cq.Vector(R_C, -BAR_L / 2.0 + hc - 0.01, ZC),
                                cq.Vector(0, 1, 0))
    cap = cq.Workplane("XY").add(c1.fuse(mid).fuse(c2).clean())
    return prof.intersect(cap)


result = core
for a in PAIR_ANGLES:
    result = result.union(make_bar().rotate((0, 0, 0), (0, 0, 1), a))

# ---------------- gaps between the two arms of each pair ----------------
R_BACK = R_OUT - NOTCH_D              # back wall of the gap: arc about the centre
for a in PAIR_ANGLES:
    box = (cq.Workplane("XY")
           .center((R_BACK - 3.0 + R_OUT + 2.0) / 2.0, 0)
           .rect(R_OUT + 2.0 - (R_BACK - 3.0), NOTCH_W)
           .extrude(H + 2.0)
           .translate((0, 0, -1.0)))
    disc = cq.Workplane("XY").circle(R_BACK).extrude(H + 4.0).translate((0, 0, -2.0))
    n = box.cut(disc)
    n = (n.edges("|Z").edges(cq.selectors.BoxSelector((R_BACK - 3.0, -NOTCH_W, -5.0),
                                                       (R_BACK + 1.0, NOTCH_W, H + 5.0)))
         .fillet(NOTCH_CR)
         .rotate((0, 0, 0), (0, 0, 1), a))
    result = result.cut(n)


def notch_edge(e):
    c = e.Center()
    for a in PAIR_ANGLES:
        u, v, z = to_local(c, a)
        if (abs(v) <= NOTCH_W / 2.0 + 0.05 and u >= R_BACK - 2.5
                and (z < H / 2.0 - 0.5 or z > H / 2.0 + 0.5 or u > R_OUT - 4.5)):
            if e.geomType() == "LINE":
                d = e.endPoint() - e.startPoint()
                if abs(d.z) > 0.9 * d.Length:
                    return False
            return True
    return False


try:
    sel = [e for e in result.edges().vals() if notch_edge(e)]
    if sel:
        result = result.newObject(sel).fillet(NOTCH_R)
except Exception:
    pass  # keep the sharp-edged gap if the round cannot be built

# ---------------- bar holes and nut traps ----------------
for a in PAIR_ANGLES:
    hole = cq.Workplane("XY").add(
        cq.Solid.makeCylinder(BAR_HOLE_D / 2.0, BAR_L + 4.0,
                              cq.Vector(R_C, -BAR_L / 2.0 - 2.0, ZC),
                              cq.Vector(0, 1, 0)))
    result = result.cut(hole.rotate((0, 0, 0), (0, 0, 1), a))
    for s in (1, -1):
        y0 = s * NOTCH_W / 2.0 - s * 0.5
        nut = (cq.Workplane("XZ", origin=(R_C, y0, ZC))
               .polygon(6, NUT_AF / math.cos(math.radians(30)))
               .extrude(-s * (NUT_DEPTH + 0.5)))
        result = result.cut(nut.rotate((0, 0, 0), (0, 0, 1), a))

# ---------------- top pockets and vertical holes ----------------
result = (result.faces(">Z").workplane(origin=(0, 0, H))
          .pushPoints([(POCKET_X, 0), (-POCKET_X, 0)])
          .hole(POCKET_D, POCKET_DEPTH))
result = (result.faces("<Z").workplane(origin=(0, 0, 0))
          .pushPoints([(POCKET_X, 0), (-POCKET_X, 0), (0, 0)])
          .hole(CENTER_HOLE_D))
pts = [(SMALL_HOLE_R * math.cos(math.radians(a)), SMALL_HOLE_R * math.sin(math.radians(a)))
       for a in (30, 150, 210, 330)]
result = (result.faces("<Z").workplane(origin=(0, 0, 0))
          .pushPoints([(x, -y) for (x, y) in pts])
          .hole(SMALL_HOLE_D))

VIEW = {"azimuth": 45, "elevation": 26}
